"""Six-armed mounting frame with claw hooks and zip-tie slots.

The plan-form is a chamfered rectangular ring with four diagonal arms and
two straight arms (offset towards +X) ending in claw hooks.  The outline is
drawn as a polygon with per-corner fillet radii (lines + tangent arcs), the
profile is extruded, then the vertical holes and zip-tie slots are cut.
"""
import math
import cadquery as cq

# ---------------------------------------------------------------- parameters
H = 21.4            # overall height (extrusion)
FW = 81.4           # frame outer half width  (X)
FH = 56.85          # frame outer half height (Y)
T = 11.1            # frame strip width (straight sides)
TC = 10.5           # frame strip width across the corner chamfers

ALPHA = 50.0        # diagonal arm angle from the X axis (deg)
YA = 43.45          # y where diagonal arm inner edge meets frame side x = -FW
ARM_W = 13.2        # diagonal arm width
ARM_L = 54.2        # chamfer face -> hook outer face, along the arm
HOOK_W = 10.5       # hook bar width
HOOK_EXT = 21.0     # hook reach past the arm inner edge
CUT_A = 22.7        # claw cut: length along the arm
CUT_B = 8.9         # claw cut: length along the hook

CX0 = 10.9          # centre arm inner (hook side) edge x
CW = 12.9           # centre arm width
CL = 54.3           # frame face -> hook outer face (centre arm)
C_HOOK_EXT = 22.0   # centre hook reach past arm inner edge
C_CUT_A = 21.3      # centre claw cut: length along the arm
C_CUT_B = 9.5       # centre claw cut: length along the hook

R_KINK = 3.0        # fillet at claw kink
R_CLAW = 6.0        # fillet at claw outer corner (diagonal arms)
R_CLAW_C = 5.0      # fillet at claw outer corner (centre arms)
R_ROOT = 5.0        # fillet at diagonal arm root (outer edge)
R_CROOT = 6.0       # fillet at centre arm root (outer edge)
R_CH = 2.0          # fillet where the outer chamfers meet the long sides
R_TIP = HOOK_W / 2  # full round hook tips

HOLE_D = 3.4        # vertical through holes in the long strips
HOLE_X = 48.5
HOLE_Y = FH - 4.0

SLOT_L = 5.6        # zip-tie slot length
SLOT_H = 1.9        # zip-tie slot height
SLOT_R = 0.5        # slot corner radius
SLOT_Z_LO = 2.9     # lower slot centre height
SLOT_Z_HI = H - 3.0 # upper slot centre height
SLOT_PITCH = 11.0   # spacing of paired slots
BOT_HOLE_D = 2.6    # small holes from underside into the slots

# ---------------------------------------------------------------- derived
a = math.radians(ALPHA)
V = (-math.cos(a), math.sin(a))     # outward direction of the (-X,+Y) arm
U = (math.sin(a), math.cos(a))      # across the arm (towards +X side)


def uv(u, v, sx=-1, sy=1):
    """local arm coords -> world xy for the arm in quadrant (sx, sy)."""
    x = u * U[0] + v * V[0]
    y = u * U[1] + v * V[1]
    return (x * -sx, y * sy)


V_CH = -FW * V[0] + YA * V[1]               # outer chamfer line (v coord)
U_IN = -FW * U[0] + YA * U[1]               # arm inner edge (u coord)
U_OUT = U_IN - ARM_W
V_TOP = V_CH + ARM_L
V_HB = V_TOP - HOOK_W
U_TIP = U_IN + HOOK_EXT
V_ROOT = (U_OUT * U[0] + FW) / -V[0]        # arm outer edge meets x = -FW
Y_ROOT = U_OUT * U[1] + V_ROOT * V[1]
XC = FW - (FH - YA) / U[1] * U[0]           # outer chamfer end on long side

IW, IH = FW - T, FH - T                     # inner opening
V_CHI = V_CH - TC
YCI = (V_CHI + IW * V[0]) / V[1]
XCI = -(V_CHI - IH * V[1]) / V[0]

CX1 = CX0 + CW
CY_TOP = FH + CL
CY_HB = CY_TOP - HOOK_W
CX_TIP = CX0 - C_HOOK_EXT


# ---------------------------------------------------------------- outline
def diag_arm_pts(sx, sy):
    """outline vertices (x, y, r) of one diagonal arm, from its root on the
    side edge round the claw to the inner corner and back to the chamfer,
    listed for the (-X,+Y) arm traversed counter-clockwise."""
    loc = [
        (U_OUT, V_ROOT, R_ROOT),            # root on the frame side
        (U_OUT, V_TOP - CUT_A, R_KINK),     # claw kink
        (U_OUT + CUT_B, V_TOP, R_CLAW),     # claw outer corner
        (U_TIP, V_TOP, R_TIP),              # hook tip
        (U_TIP, V_HB, R_TIP),
        (U_IN, V_HB, 0.0),                  # hook inner corner
        (U_IN, V_CH, 0.0),                  # arm meets chamfer
    ]
    # traversal above is clockwise for (-X,+Y); reverse it to go CCW
    pts = [uv(u, v, sx, sy) + (r,) for (u, v, r) in reversed(loc)]
    if sx * sy > 0:                          # mirrored once -> flip order
        pts = pts[::-1]
    return pts


def centre_arm_pts(sy):
    loc = [
        (CX1, FH, R_CROOT),
        (CX1, CY_TOP - C_CUT_A, R_KINK),
        (CX1 - C_CUT_B, CY_TOP, R_CLAW_C),
        (CX_TIP, CY_TOP, R_TIP),
        (CX_TIP, CY_HB, R_TIP),
        (CX0, CY_HB, 0.0),
        (CX0, FH, 0.0),
    ]
    pts = [(x, y * sy, r) for (x, y, r) in loc]
    if sy < 0:
        pts = pts[::-1]
    return pts


def outline():
    pts = []
    # bottom side, left to right: (-X,-Y) chamfer end ... centre arm ...
    pts += [(-XC, -FH, R_CH)]
    pts += centre_arm_pts(-1)
    pts += [(XC, -FH, R_CH)]
    pts += diag_arm_pts(1, -1)               # (+X,-Y) arm
    pts += diag_arm_pts(1, 1)                # (+X,+Y) arm
    pts += [(XC, FH, R_CH)]
    pts += centre_arm_pts(1)
    pts += [(-XC, FH, R_CH)]
    pts += diag_arm_pts(-1, 1)               # (-X,+Y) arm
    pts += diag_arm_pts(-1, -1)              # (-X,-Y) arm
    return pts


def _unit(x, y):
    l = math.hypot(x, y)
    return (x / l, y / l)


def filleted_edges(verts):
    """closed polygon [(x, y, r), ...] -> list of cq.Edge (lines and tangent
    fillet arcs; r = 0 keeps the corner sharp)."""
    n = len(verts)
    corner = []
    for i in range(n):
        px, py, r = verts[i]
        qx, qy, _ = verts[i - 1]
        nx, ny, _ = verts[(i + 1) % n]
        din = _unit(px - qx, py - qy)
        dout = _unit(nx - px, ny - py)
        if r <= 0:
            corner.append(((px, py), None, (px, py)))
            continue
        cr = din[0] * dout[1] - din[1] * dout[0]
        ang = math.acos(max(-1.0, min(1.0, din[0] * dout[0] + din[1] * dout[1])))
        tl = r * math.tan(ang / 2)
        tin = (px - din[0] * tl, py - din[1] * tl)
        tout = (px + dout[0] * tl, py + dout[1] * tl)
        s = 1.0 if cr > 0 else -1.0
        cx, cy = tin[0] - din[1] * r * s, tin[1] + din[0] * r * s
        m = _unit(px - cx, py - cy)
        corner.append((tin, (cx + m[0] * r, cy + m[1] * r), tout))

    v3 = lambda p: cq.Vector(p[0], p[1], 0)
    edges = []
    for i in range(n):
        tin, mid, tout = corner[i]
        if mid is not None:
            edges.append(cq.Edge.makeThreePointArc(v3(tin), v3(mid), v3(tout)))
        nxt = corner[(i + 1) % n][0]
        if math.hypot(nxt[0] - tout[0], nxt[1] - tout[1]) > 1e-7:
            edges.append(cq.Edge.makeLine(v3(tout), v3(nxt)))
    return edges


outer_wire = cq.Wire.assembleEdges(filleted_edges(outline()))
inner_pts = [(-IW, -YCI), (-XCI, -IH), (XCI, -IH), (IW, -YCI),
             (IW, YCI), (XCI, IH), (-XCI, IH), (-IW, YCI)]
inner_wire = cq.Wire.makePolygon([cq.Vector(x, y, 0) for x, y in inner_pts], close=True)
face = cq.Face.makeFromWires(outer_wire, [inner_wire])
body = cq.Solid.extrudeLinear(face, cq.Vector(0, 0, H))
result = cq.Workplane("XY").add(body)

# ---------------------------------------------------------------- holes & slots
def slot_cutter(cx, cy, z, dirx, diry, length):
    """horizontal rounded-rectangle slot centred at (cx,cy,z), through along (dirx,diry)."""
    n = cq.Vector(dirx, diry, 0).normalized()
    xd = cq.Vector(-diry, dirx, 0).normalized()
    pl = cq.Plane(origin=(cx - n.x * length / 2, cy - n.y * length / 2, z),
                  xDir=xd, normal=n)
    sk = cq.Sketch().rect(SLOT_L, SLOT_H).vertices().fillet(SLOT_R)
    return cq.Workplane(pl).placeSketch(sk).extrude(length)


def bottom_hole(cx, cy, z):
    return cq.Workplane("XY").center(cx, cy).circle(BOT_HOLE_D / 2).extrude(z)


cutters = []
# vertical through holes in the long strips
for sx in (-1, 1):
    for sy in (-1, 1):
        cutters.append(cq.Workplane("XY").center(HOLE_X * sx, HOLE_Y * sy)
                       .circle(HOLE_D / 2).extrude(H))
for sy in (-1, 1):
    yc = (FH - T / 2) * sy
    # stacked slot pair under each top hole
    for sx in (-1, 1):
        for z in (SLOT_Z_LO, SLOT_Z_HI):
            cutters.append(slot_cutter(HOLE_X * sx, yc, z, 0, 1, T + 2))
    # bottom pair in the strip and in the centre hook
    yh = (CY_TOP - HOOK_W / 2) * sy
    for dx in (-SLOT_PITCH / 2, SLOT_PITCH / 2):
        cutters.append(slot_cutter(dx, yc, SLOT_Z_LO, 0, 1, T + 2))
        cutters.append(bottom_hole(dx, yc, SLOT_Z_LO))
        cutters.append(slot_cutter(dx, yh, SLOT_Z_LO, 0, 1, HOOK_W + 2))
        cutters.append(bottom_hole(dx, yh, SLOT_Z_LO))

# diagonal corners: slot pairs through the chamfer strip and through the hook
U_C = (U_IN + U_TIP) / 2.0
for sx in (-1, 1):
    for sy in (-1, 1):
        vx, vy = V[0] * -sx, V[1] * sy
        for du in (-SLOT_PITCH / 2, SLOT_PITCH / 2):
            for vc, th in ((V_CH - TC / 2, TC), (V_TOP - HOOK_W / 2, HOOK_W)):
                cx, cy = uv(U_C + du, vc, sx, sy)
                cutters.append(slot_cutter(cx, cy, SLOT_Z_LO, vx, vy, th + 2))
                cutters.append(bottom_hole(cx, cy, SLOT_Z_LO))

tool = cutters[0]
for c in cutters[1:]:
    tool = tool.union(c)
result = result.cut(tool)

VIEW = {"azimuth": 45, "elevation": 26}
